import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
AX = -0.9            # Y of the common axis (bar, straps, knuckles, dish)

# vertical bar (separate body)
BAR_T = 2.6          # thickness (X) of the long bar
BAR_W = 11.0         # width (Y) of the long bar
TAB_T = 7.5          # thickness (X) of the bottom lug
TAB_W = 15.6         # width (Y) of the bottom lug
TAB_H = 19.8         # height of the straight part of the lug
TAPER_W_TOP = 36.0   # z where the width taper ends
TAPER_T_MID = 36.0   # z where the steep thickness taper ends
TAPER_T_TOP = 58.0   # z where the thickness reaches BAR_T
HOLE_D = 7.0         # hole in the lug
HOLE_Z = 7.3
SHOULDER_Z = 129.4   # top of the bar shoulders
BAR_TOP = 133.4      # top of the centre tongue
TONGUE_W = 3.6

# clip body
Z0 = 129.2           # underside of straps / box
STRAP_T = 3.2
STRAP_W = 11.6
STRAP_X0 = 7.2
BOX_X0, BOX_X1 = 29.5, 54.8
BOX_W = 26.8         # box length in Y
FLOOR_TOP = 133.3
WALL_T = 2.2
WALL_TOP = 139.0     # top of the side walls
POST_TOP = 140.0     # top of the corner posts
POST_D = 3.8
POST_X_IN = 0.8      # post centre measured from the outer wall face
POST_Y = 11.2
DISH_D = 13.4
DISH_D2 = 9.5
DISH_DEPTH = 1.6
LOOP_OUT_X = 23.2    # outer face of the -X loop
LOOP_TOP = 133.6
LOOP_BAR = 2.0
WIN_HALF = 7.35      # half length of the loop window
KNUCKLE_D = 3.6
KNUCKLE_X = 28.1
KNUCKLE_Y = 10.05
KNUCKLE_TOP = 135.6
BULB_TOP = 136.8
PIN_D = 1.7
STRAP2_X1 = 70.0

# cover plate (separate body)
PL_X0, PL_X1 = 73.2, 100.0
PL_W = 26.8
PL_Z0 = 139.8
PL_T = 1.8
RIM_H = 2.3
RIM_INSET = 1.5
NOTCH_X = 83.2
NOTCH_R = 4.9
NOTCH_DEPTH = 8.5

XC = (BOX_X0 + BOX_X1) / 2.0   # centre of the box in X


def box_at(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_z(x, y, d, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(d / 2.0).extrude(z1 - z0))


# ================= bar =================
def make_bar():
    # side profile (XZ) extruded along Y
    side = (cq.Workplane("XZ")
            .moveTo(0, 0).lineTo(TAB_T, 0).lineTo(TAB_T, TAB_H)
            # one smooth curve from the lug up to the top of the bar
            .spline([(BAR_T + 1.1, TAPER_T_MID), (BAR_T + 0.2, TAPER_T_TOP - 6),
                     (BAR_T + 0.02, 85.0), (BAR_T, BAR_TOP)],
                    tangents=[(-0.22, 1), (0, 1)], includeCurrent=True)
            .lineTo(0, BAR_TOP).close()
            .extrude(-(TAB_W + 1.0)).translate((0, AX - TAB_W / 2 - 0.5, 0)))
    hw, tw = BAR_W / 2, TAB_W / 2
    face = (cq.Workplane("YZ")
            .moveTo(AX - tw, 0).lineTo(AX + tw, 0).lineTo(AX + tw, TAB_H)
            .spline([(AX + hw, TAPER_W_TOP)], tangents=[(-0.25, 1), (0, 1)],
                    includeCurrent=True)
            .lineTo(AX + hw, SHOULDER_Z)
            .lineTo(AX + TONGUE_W / 2, SHOULDER_Z)
            .lineTo(AX + TONGUE_W / 2, BAR_TOP)
            .lineTo(AX - TONGUE_W / 2, BAR_TOP)
            .lineTo(AX - TONGUE_W / 2, SHOULDER_Z)
            .lineTo(AX - hw, SHOULDER_Z)
            .lineTo(AX - hw, TAPER_W_TOP)
            .spline([(AX - tw, TAB_H)], tangents=[(0, -1), (-0.25, -1)],
                    includeCurrent=True)
            .close()
            .extrude(TAB_T + 1.0).translate((-0.5, 0, 0)))
    bar = side.intersect(face)
    bar = bar.edges("|Y and >Z").fillet(0.8)
    hole = (cq.Workplane("YZ").center(AX, HOLE_Z).circle(HOLE_D / 2)
            .extrude(TAB_T + 2.0).translate((-1.0, 0, 0)))
    return bar.cut(hole)


# ================= clip body =================
def loop_half(side):
    """D-shaped loop ring with two hinge knuckles on one side of the box."""
    m = -1 if side < 0 else 1

    def mx(x):  # mirror an x coordinate about the box centre for the +X side
        return x if side < 0 else 2 * XC - x

    xo, xi = mx(LOOP_OUT_X), mx(BOX_X0 + 0.6)
    outer = [(xi, AX - 12.0), (mx(KNUCKLE_X - 1.6), AX - 12.0),
             (xo, AX - 8.4), (xo, AX + 8.4),
             (mx(KNUCKLE_X - 1.6), AX + 12.0), (xi, AX + 12.0)]
    ring = (cq.Workplane("XY").workplane(offset=Z0).polyline(outer).close()
            .extrude(LOOP_TOP - Z0))
    ring = ring.edges("|Z").fillet(1.0)
    wa, wb = mx(LOOP_OUT_X + LOOP_BAR), mx(BOX_X0 + 1.5)
    win = box_at(min(wa, wb), max(wa, wb), AX - WIN_HALF, AX + WIN_HALF,
                 Z0 - 1, LOOP_TOP + 1)
    win = win.edges("|Z").fillet(0.8)
    ring = ring.cut(win)
    # round the exposed top edges of the ring (not the ones against the box)
    xa, xb = mx(LOOP_OUT_X - 1.0), mx(BOX_X0 - 0.3)
    sel = cq.selectors.BoxSelector((min(xa, xb), AX - 20, LOOP_TOP - 0.1),
                                   (max(xa, xb), AX + 20, LOOP_TOP + 0.1))
    ring = ring.edges(sel).fillet(0.6)
    for sy in (-1, 1):
        kx, ky = mx(KNUCKLE_X), AX + sy * KNUCKLE_Y
        kn = cyl_z(kx, ky, KNUCKLE_D, Z0, LOOP_TOP + 0.2)
        # sloped bulb that blends the knuckle into the tall corner post
        px = BOX_X0 + POST_X_IN if side < 0 else BOX_X1 - POST_X_IN
        py = sy * POST_Y
        dx, dy = 0.6 * (px - kx), 0.6 * (py - ky)
        cap = (cq.Workplane("XY").workplane(offset=LOOP_TOP + 0.2)
               .center(kx, ky).circle(KNUCKLE_D / 2)
               .workplane(offset=BULB_TOP - LOOP_TOP - 0.2)
               .center(dx, dy).circle(POST_D / 2 - 0.5).loft())
        ring = ring.union(kn).union(cap)
    return ring


def make_clip():
    zt = Z0 + STRAP_T
    # ---- left strap with window and small pocket
    strap = box_at(STRAP_X0, LOOP_OUT_X + 0.5, AX - STRAP_W / 2,
                   AX + STRAP_W / 2, Z0, zt)
    strap = strap.edges("|Y and <X").fillet(1.4)
    strap = strap.faces(">Z").edges("|X").fillet(0.7)
    strap = strap.cut(box_at(10.3, LOOP_OUT_X + 0.01, AX - 4.35, AX + 4.35,
                             Z0 - 1, zt + 1).edges("|Z").fillet(0.5))
    strap = strap.cut(box_at(7.9, 9.7, AX - 2.4, AX + 2.4, zt - 1.2, zt + 1))

    # ---- right short strap
    x2 = 2 * XC - LOOP_OUT_X
    strap2 = box_at(x2 - 0.5, STRAP2_X1, AX - STRAP_W / 2, AX + STRAP_W / 2,
                    Z0, zt)
    strap2 = strap2.edges("|Z and >X").fillet(1.0)
    strap2 = strap2.faces(">Z").edges("|X").fillet(0.7)
    strap2 = strap2.cut(box_at(x2 - 0.01, 66.2, AX - 4.15, AX + 4.15,
                               Z0 - 1, zt + 1).edges("|Z").fillet(0.5))
    strap2 = strap2.cut(box_at(66.9, 68.8, AX - 2.2, AX + 2.2, zt - 1.2, zt + 1))

    # ---- box: floor + two walls (U channel) + corner posts
    floor = box_at(BOX_X0, BOX_X1, -BOX_W / 2, BOX_W / 2, Z0, FLOOR_TOP)
    for xw0 in (BOX_X0, BOX_X1 - WALL_T):
        floor = floor.union(box_at(xw0, xw0 + WALL_T, -BOX_W / 2, BOX_W / 2,
                                   Z0, WALL_TOP))
    body = floor.edges("|Z").fillet(1.0)
    body = body.edges("<Z").fillet(1.2)
    for px in (BOX_X0 + POST_X_IN, BOX_X1 - POST_X_IN):
        for sy in (-1, 1):
            post = cyl_z(px, sy * POST_Y, POST_D, Z0 + 1.3, POST_TOP)
            post = post.faces(">Z").edges().fillet(0.6)
            body = body.union(post)

    # dish in the floor
    dish = (cq.Workplane("XY").workplane(offset=FLOOR_TOP - DISH_DEPTH)
            .center(XC, AX).circle(DISH_D2 / 2)
            .workplane(offset=DISH_DEPTH).circle(DISH_D / 2).loft())
    body = body.cut(dish)

    # latch recesses at the top of the inner wall faces, with a small ramp
    for xin, sgn in ((BOX_X0 + WALL_T, 1), (BOX_X1 - WALL_T, -1)):
        xa, xb = (xin - 1.2, xin + 0.01) if sgn > 0 else (xin - 0.01, xin + 1.2)
        body = body.cut(box_at(xa, xb, AX - 3.8, AX + 3.8, 137.2, WALL_TOP + 1))
        xback = xin - sgn * 1.2
        ramp = (cq.Workplane("XZ")
                .polyline([(xback - sgn * 0.1, 137.2), (xin + sgn * 0.4, 137.2),
                           (xback - sgn * 0.1, 138.7)]).close()
                .extrude(-7.0).translate((0, AX - 3.5, 0)))
        body = body.union(ramp)

    # loops with knuckles on both sides, then pin holes
    body = body.union(loop_half(-1)).union(loop_half(1))
    for kx in (KNUCKLE_X, 2 * XC - KNUCKLE_X):
        for sy in (-1, 1):
            body = body.cut(cyl_z(kx, AX + sy * KNUCKLE_Y, PIN_D, Z0 - 1,
                                  KNUCKLE_TOP + 1))

    return body.union(strap).union(strap2)


# ================= plate =================
SLANT = 0.36          # x shift of the slot ends per mm of -y
# (x_left, x_right_at_top, y_centre, width, left_end) ; left_end: 'key' or 'round'
SLOTS = [(79.6, 91.1, 0.6, 2.4, "key"),
         (78.3, 87.0, -3.6, 2.7, "round_both"),
         (89.5, 93.0, -3.6, 2.7, "round"),
         (79.6, 94.1, -7.9, 2.6, "key")]
KEY_D = 3.6


def slot_solid(xl, xr, y, w, kind, grow, z0, h):
    r = w / 2 + grow
    yt, yb = y + r, y - r
    if kind == "round_both":
        sk = (cq.Workplane("XY").workplane(offset=z0)
              .center((xl + xr) / 2, y).slot2D(xr - xl + 2 * grow, 2 * r))
        return sk.extrude(h)
    xrt = xr + grow
    xrb = xrt + SLANT * 2 * r
    body = (cq.Workplane("XY").workplane(offset=z0)
            .polyline([(xl, yb), (xrb, yb), (xrt, yt), (xl, yt)]).close()
            .extrude(h))
    d = KEY_D + 2 * grow if kind == "key" else 2 * r
    return body.union(cyl_z(xl, y, d, z0, z0 + h))


def make_plate():
    yc = 0.0
    zt = PL_Z0 + PL_T
    top = box_at(PL_X0, PL_X1, yc - PL_W / 2, yc + PL_W / 2, PL_Z0, zt)
    top = top.edges("|Z").fillet(2.5)
    # U notch on the +Y edge with rounded entry corners
    ny = yc + PL_W / 2 - NOTCH_DEPTH + NOTCH_R
    notch = cyl_z(NOTCH_X, ny, 2 * NOTCH_R, PL_Z0 - 5, zt + 5).union(
        box_at(NOTCH_X - NOTCH_R, NOTCH_X + NOTCH_R, ny, ny + 10,
               PL_Z0 - 5, zt + 5))
    top = top.cut(notch)
    top = top.edges("|Z").edges(cq.selectors.BoxSelector(
        (NOTCH_X - NOTCH_R - 0.5, yc + PL_W / 2 - 0.5, PL_Z0 - 1),
        (NOTCH_X + NOTCH_R + 0.5, yc + PL_W / 2 + 0.5, zt + 1))).fillet(2.0)
    top = top.faces(">Z").edges().fillet(0.8)

    # underside rim with gaps on the +/-X sides
    rim = box_at(PL_X0 + RIM_INSET, PL_X1 - RIM_INSET,
                 yc - PL_W / 2 + RIM_INSET, yc + PL_W / 2 - RIM_INSET,
                 PL_Z0 - RIM_H, PL_Z0 + 0.1)
    rim = rim.edges("|Z").fillet(1.5)
    rim = rim.cut(box_at(PL_X0 + RIM_INSET + 1.1, PL_X1 - RIM_INSET - 1.1,
                         yc - PL_W / 2 + RIM_INSET + 1.1,
                         yc + PL_W / 2 - RIM_INSET - 1.1,
                         PL_Z0 - RIM_H - 1, PL_Z0 + 0.05))
    rim = rim.cut(box_at(PL_X0, PL_X1, AX - 3.8, AX + 3.8,
                         PL_Z0 - RIM_H - 1, PL_Z0 - 0.6))
    rim = rim.cut(cyl_z(NOTCH_X, ny, 2 * NOTCH_R + 2.2, PL_Z0 - 5, PL_Z0 + 0.05))
    rim = rim.cut(box_at(NOTCH_X - NOTCH_R - 1.1, NOTCH_X + NOTCH_R + 1.1, ny,
                         ny + 10, PL_Z0 - 5, PL_Z0 + 0.05))
    # frame around the slot field on the underside
    fr = box_at(76.6, 97.0, -10.4, 2.9, PL_Z0 - 1.4, PL_Z0 + 0.1)
    fr = fr.cut(box_at(77.4, 96.2, -9.6, 2.1, PL_Z0 - 2, PL_Z0 + 0.05))
    plate = top.union(rim).union(fr)

    # keyhole slots
    for xl, xr, y, w, kind in SLOTS:
        plate = plate.cut(slot_solid(xl, xr, y, w, kind, 0.0, PL_Z0 - 5, 10))

    # small nubs on the +Y edge corners
    for nx in (75.6, 96.8):
        nub = (cq.Workplane("YZ").workplane(offset=nx - 1.1)
               .center(yc + PL_W / 2 - 0.9, zt - 0.3).circle(0.75).extrude(2.2))
        plate = plate.union(nub)
    return plate


bar = make_bar()
clip = make_clip()
plate = make_plate()

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(
    [bar.val(), clip.val(), plate.val()])])

VIEW = {"azimuth": 45, "elevation": 26}
